import cadquery as cq

# =====================================================================
#  Open-top electronics tray / drive-bay style box
#  origin: front-left-bottom outer corner, X = width, Y = depth, Z = up
# =====================================================================

# ============ main dimensions (mm) ============
L = 150.0      # X width
W = 101.0      # Y depth of main box
H = 35.6       # Z height
T = 2.2        # outer wall thickness
TF = 1.0       # base floor thickness
TAB_W = 25.5   # back-left tab width (X)
TAB_D = 13.9   # tab extension behind main back wall (Y)

# floor frame (thicker plate around the window) and window
FR_X0, FR_X1 = 35.5, 124.9
FR_Y0, FR_Y1 = 5.6, 91.9
FR_STEP_X, FR_STEP_Y = 95.7, 87.0      # back-right corner of frame cut back
FR_T = 2.3                              # frame thickness
FR_RIB_X1, FR_RIB_Y0 = 136.6, 85.0      # thin rib continuing the frame's back edge
OP_X0, OP_X1 = 43.7, 115.7              # through window
OP_Y0, OP_Y1 = 13.4, 85.5
REC_M = 3.0                             # underside groove outer margin around window
REC_IN = 1.0                            # underside groove inner margin (full-thickness lip)
REC_D = 1.2                             # underside groove depth
REC_D0 = 0.4                            # underside shallow recess under the frame

# inner guide walls (along Y, near the -X side) with notched tops
GW_T = 3.4
GW1_X = 2.6
GW2_X = 15.2
GW_TOP = 29.9
GW1_YEND = 97.3
NOTCHES = [(18.8, 30.3), (67.3, 78.5)]
NOTCH_FLOOR = 24.3
GW_HOLE_Y = [14.2, 35.0, 62.35, 83.1]
GW_HOLE_Z = 25.3
GW_HOLE_D = 2.7

# back end of the guide walls / tab compartment
CR_Y0 = 96.2          # cross rib (right of wall 2) front face
CR_X1 = 30.0          # cross rib end
DIV_X0 = 16.1         # tab filler block -X face
END_Y0, END_Y1 = 95.1, 97.5
END1_X1 = 8.9         # end block on wall 1
END2_X0 = 12.6        # end block on wall 2
CHAN_Z = 20.0         # low cross piece closing the channel between walls

# V-groove along the +X face of guide wall 2
GRV_Z0, GRV_Z1 = 3.7, 11.1     # groove mouth on the wall face (bottom / top)
GRV_D = 2.0                    # groove depth into the wall
GRV_ZF = 8.2                   # top of the sloped lower flank
GRV_Y1 = 94.0                  # groove ends here (front of guide post)

# guide posts at the groove end
POST_Y0 = 94.0
POSTA_W, POSTA_Z = 2.6, 12.0
POSTB_X0, POSTB_X1, POSTB_Z = 24.2, 27.6, 12.3

# back wall features
BOSS = (109.6, 121.3, 96.5, 26.6, 30.0)          # x0, x1, y0, z0, z1
BRACKET = (96.7, 101.2, 96.6, 2.1, 4.6)          # x0, x1, y0, z0, z1
BSLOT_X0, BSLOT_X1, BSLOT_Z, BSLOT_W = 49.2, 94.1, 22.3, 3.5
BWIN_X, BWIN_Z, BWIN_W, BWIN_H, BWIN_R = 49.4, 7.3, 9.0, 6.0, 1.6

# floor slots near back wall
FSLOT1 = (57.5, 66.5, 94.3, 96.5)
FSLOT2_X0, FSLOT2_X1, FSLOT2_Y, FSLOT2_W = 93.5, 102.1, 95.1, 2.0

# clips along the right edge of the frame
CLIP_X1 = 129.4
CLIP1_Y1, CLIP1_Z = 14.5, 13.2
CLIP_CYL_Y1, CLIP_CYL_R, CLIP_CYL_Z = 23.8, 2.2, 3.4
CLIP2_Y0, CLIP2_Y1, CLIP2_Z = 49.3, 74.6, 6.0

# card slot in the front wall, and its housing behind the wall
HOUS_X0, HOUS_X1, HOUS_Z = 24.3, 128.5, 10.1
FREC = (34.5, 124.4, 3.4, 4.5, 8.7)              # x0, x1, depth(y), z0, z1
FSLOT = (37.0, 122.2, 5.0, 5.0, 6.6)
FPOCKETS_X = [(43.8, 52.3), (107.4, 115.9)]
FPOCKET_Z = (0.6, 3.2)

# -X wall: long thin slot near bottom
LSLOT_Y0, LSLOT_Y1 = 4.8, 94.2
LSLOT_Z, LSLOT_H = 9.4, 2.0

# tab back face: larger countersunk hole
TAB_HOLE_X, TAB_HOLE_Z, TAB_HOLE_R, TAB_CS_R = 11.5, 13.3, 1.8, 3.3

# countersunk screw holes near top edge of outer walls
CS_D = 2.2
CS_DK = 4.6
FRONT_HOLES_X = [28.6, 74.8, 126.7]
FRONT_HOLE_Z = 33.2
RIGHT_HOLES_Y = [33.1, 67.9]
RIGHT_HOLE_Z = 33.3
LEFT_HOLES_Y = [34.3, 80.5]
LEFT_HOLE_Z = 33.2
BACK_HOLES_X = [63.7, 109.6]
BACK_HOLE_Z = 33.2
TAB_TOP_HOLE_X, TAB_TOP_HOLE_Z = 12.8, 33.0

VIEW = {"azimuth": 45, "elevation": 26}

WALL_IN_Y = W - T          # inner face of main back wall
TAB_IN_Y = W + TAB_D - T   # inner face of tab back wall
E = 0.01                   # small overlap for clean unions


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ============ outer shell ============
pts_out = [(0, 0), (L, 0), (L, W), (TAB_W, W), (TAB_W, W + TAB_D), (0, W + TAB_D)]
pts_in = [(T, T), (L - T, T), (L - T, W - T), (TAB_W - T, W - T),
          (TAB_W - T, TAB_IN_Y), (T, TAB_IN_Y)]
body = cq.Workplane("XY").polyline(pts_out).close().extrude(H)
cavity = (cq.Workplane("XY").workplane(offset=TF)
          .polyline(pts_in).close().extrude(H))
body = body.cut(cavity)

# ============ floor frame + window ============
frame_pts = [(FR_X0, FR_Y0), (FR_X1, FR_Y0), (FR_X1, FR_STEP_Y),
             (FR_STEP_X, FR_STEP_Y), (FR_STEP_X, FR_Y1), (FR_X0, FR_Y1)]
body = body.union(cq.Workplane("XY").polyline(frame_pts).close().extrude(FR_T))
body = body.union(box(FR_X1 - E, FR_RIB_X1, FR_RIB_Y0, FR_STEP_Y, TF - E, FR_T))

body = body.cut(box(OP_X0, OP_X1, OP_Y0, OP_Y1, -1, FR_T + 1))
# underside: shallow recess under the frame + groove ring around the window
body = body.cut(box(FR_X0 + 1.5, FR_X1 - 1.5, FR_Y0 + 1.5, FR_Y1 - 1.5, -1, REC_D0))
rec_y1 = min(OP_Y1 + REC_M, FR_STEP_Y - 0.8)
rec_ring = (box(OP_X0 - REC_M, OP_X1 + REC_M, OP_Y0 - REC_M, rec_y1, -1, REC_D)
            .cut(box(OP_X0 - REC_IN, OP_X1 + REC_IN, OP_Y0 - REC_IN, OP_Y1 + REC_IN,
                     -2, REC_D + 1)))
body = body.cut(rec_ring)

# ============ guide walls with notched tops ============
for gx, gy1 in ((GW1_X, GW1_YEND), (GW2_X, WALL_IN_Y + E)):
    wall = box(gx, gx + GW_T, T - E, gy1, TF - E, GW_TOP)
    for (n0, n1) in NOTCHES:
        wall = wall.cut(box(gx - 1, gx + GW_T + 1, n0, n1, NOTCH_FLOOR, GW_TOP + 1))
    body = body.union(wall)

gx_face = GW2_X + GW_T     # +X face of guide wall 2

# cross rib right of wall 2, filler block in the tab, end blocks, channel closer
body = body.union(box(gx_face - E, CR_X1, CR_Y0, WALL_IN_Y + E, TF - E, GW_TOP))
body = body.union(box(DIV_X0, TAB_W - T + E, WALL_IN_Y - E, TAB_IN_Y + E, TF - E, GW_TOP))
body = body.union(box(END2_X0, GW2_X + E, END_Y0, END_Y1, TF - E, GW_TOP))
body = body.union(box(GW1_X + GW_T - E, END1_X1, END_Y0, GW1_YEND, TF - E, GW_TOP))
body = body.union(box(GW1_X + GW_T - E, GW2_X + E, END_Y0, END_Y1, TF - E, CHAN_Z))

# holes through both guide walls
for hy in GW_HOLE_Y:
    cyl = (cq.Workplane("YZ").workplane(offset=GW1_X - 1)
           .center(hy, GW_HOLE_Z).circle(GW_HOLE_D / 2).extrude(gx_face - GW1_X + 2))
    body = body.cut(cyl)

# V-groove in +X face of guide wall 2 (sloped lower flank, flat upper face)
grv_k = (GRV_ZF - GRV_Z0) / GRV_D
groove = (cq.Workplane("XZ")
          .polyline([(gx_face + 0.5, GRV_Z0 - 0.5 * grv_k),
                     (gx_face - GRV_D, GRV_ZF),
                     (gx_face - GRV_D, GRV_Z1),
                     (gx_face + 0.5, GRV_Z1)])
          .close()
          .extrude(-(GRV_Y1 - T + 1)).translate((0, T - 1, 0)))
body = body.cut(groove)

# guide posts at the groove end
body = body.union(box(gx_face - E, gx_face + POSTA_W, POST_Y0, CR_Y0 + E, TF - E, POSTA_Z))
body = body.union(box(POSTB_X0, POSTB_X1, POST_Y0, CR_Y0 + E, TF - E, POSTB_Z))

# ============ back wall and floor details ============
bx0, bx1, by0, bz0, bz1 = BOSS
body = body.union(box(bx0, bx1, by0, WALL_IN_Y + E, bz0, bz1))
kx0, kx1, ky0, kz0, kz1 = BRACKET
body = body.union(box(kx0, kx1, ky0, WALL_IN_Y + E, kz0, kz1))

body = body.cut(box(FSLOT1[0], FSLOT1[1], FSLOT1[2], FSLOT1[3], -1, FR_T + 1))
body = body.cut(cq.Workplane("XY").center((FSLOT2_X0 + FSLOT2_X1) / 2, FSLOT2_Y)
                .slot2D(FSLOT2_X1 - FSLOT2_X0, FSLOT2_W, 0)
                .extrude(FR_T + 2).translate((0, 0, -1)))

# clips / stops at the right edge of the frame, relief pockets underneath
body = body.union(box(FR_X1 - E, CLIP_X1, FR_Y0 - E, CLIP1_Y1, TF - E, CLIP1_Z))
clip_cyl = (cq.Workplane("XZ").workplane(offset=-(CLIP1_Y1 - 0.1))
            .center((FR_X1 + CLIP_X1) / 2, CLIP_CYL_Z).circle(CLIP_CYL_R)
            .extrude(-(CLIP_CYL_Y1 - CLIP1_Y1 + 0.1)))
body = body.union(clip_cyl)
body = body.union(box(FR_X1 - E, CLIP_X1, CLIP2_Y0, CLIP2_Y1, TF - E, CLIP2_Z))
body = body.cut(box(FR_X1 + 0.7, CLIP_X1 - 0.7, CLIP1_Y1 + 0.8, CLIP_CYL_Y1 - 0.7, -1, 0.6))
body = body.cut(box(FR_X1 + 0.7, CLIP_X1 - 0.7, CLIP2_Y0 + 0.7, CLIP2_Y1 - 0.7, -1, 0.6))

# card-slot housing behind the front wall
body = body.union(box(HOUS_X0, HOUS_X1, T - E, FR_Y0 + E, TF - E, HOUS_Z))

# back wall: long slot and rounded-rect window
slot_back = (cq.Workplane("XZ").workplane(offset=-(W + 1))
             .center((BSLOT_X0 + BSLOT_X1) / 2, BSLOT_Z)
             .slot2D(BSLOT_X1 - BSLOT_X0, BSLOT_W, 0).extrude(T + 2))
body = body.cut(slot_back)
rr = (cq.Workplane("XZ").workplane(offset=-(W + 1))
      .sketch().rect(BWIN_W, BWIN_H).vertices().fillet(BWIN_R).finalize()
      .extrude(T + 2).translate((BWIN_X, 0, BWIN_Z)))
body = body.cut(rr)

# -X wall: long thin slot near bottom
body = body.cut(box(-1, T + 0.2, LSLOT_Y0, LSLOT_Y1,
                    LSLOT_Z - LSLOT_H / 2, LSLOT_Z + LSLOT_H / 2))

# tab back face: larger countersunk hole in the middle
body = body.cut(cq.Workplane("XZ").workplane(offset=-(W + TAB_D + 1))
                .center(TAB_HOLE_X, TAB_HOLE_Z).circle(TAB_HOLE_R).extrude(T + 2))
body = body.cut(cq.Workplane("XZ").workplane(offset=-(W + TAB_D))
                .center(TAB_HOLE_X, TAB_HOLE_Z).circle(TAB_CS_R)
                .workplane(offset=TAB_CS_R - TAB_HOLE_R).circle(TAB_HOLE_R).loft())

# front wall: recessed card slot with two small pockets below
fx0, fx1, fd, fz0, fz1 = FREC
body = body.cut(box(fx0, fx1, -1, fd, fz0, fz1))
sx0, sx1, sd, sz0, sz1 = FSLOT
body = body.cut(box(sx0, sx1, -1, sd, sz0, sz1))
for (px0, px1) in FPOCKETS_X:
    body = body.cut(box(px0, px1, -1, 0.8, FPOCKET_Z[0], FPOCKET_Z[1]))


# ============ countersunk holes near the top edge ============
CS_H = (CS_DK - CS_D) / 2      # 90 degree countersink depth


def cs_y(x, z, y_face, into):
    """countersunk hole in a wall parallel to XZ; into = +1 / -1 along Y"""
    # XZ workplane normal is -Y, so workplane offset o sits at y = -o
    thru = (cq.Workplane("XZ").workplane(offset=-(y_face - into))
            .center(x, z).circle(CS_D / 2).extrude(-into * (T + 2)))
    cone = (cq.Workplane("XZ").workplane(offset=-y_face)
            .center(x, z).circle(CS_DK / 2)
            .workplane(offset=-into * CS_H).circle(CS_D / 2).loft())
    return thru.union(cone)


def cs_x(y, z, x_face, into):
    """countersunk hole in a wall parallel to YZ; into = +1 / -1 along X"""
    thru = (cq.Workplane("YZ").workplane(offset=x_face - into)
            .center(y, z).circle(CS_D / 2).extrude(into * (T + 2)))
    cone = (cq.Workplane("YZ").workplane(offset=x_face)
            .center(y, z).circle(CS_DK / 2)
            .workplane(offset=into * CS_H).circle(CS_D / 2).loft())
    return thru.union(cone)


for hx in FRONT_HOLES_X:
    body = body.cut(cs_y(hx, FRONT_HOLE_Z, 0.0, +1))
for hx in BACK_HOLES_X:
    body = body.cut(cs_y(hx, BACK_HOLE_Z, W, -1))
body = body.cut(cs_y(TAB_TOP_HOLE_X, TAB_TOP_HOLE_Z, W + TAB_D, -1))
for hy in RIGHT_HOLES_Y:
    body = body.cut(cs_x(hy, RIGHT_HOLE_Z, L, -1))
for hy in LEFT_HOLES_Y:
    body = body.cut(cs_x(hy, LEFT_HOLE_Z, 0.0, +1))

result = body
